import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# box (open toward -Y, back closed by the plate)
BOX_W = 69.0        # X
BOX_H = 43.5        # Z
BOX_D = 44.0        # Y (front face at Y=0, plate front face at Y=BOX_D)
WALL_L = 3.5
WALL_R = 3.0
WALL_T = 2.5
WALL_B = 2.5
BOX_C = 1.9         # outer edge chamfer
CAV_D = 38.8        # depth of the cavity (back wall is thicker than the plate)

# back plate
PLATE_T = 3.5
PY0 = BOX_D
PY1 = BOX_D + PLATE_T

# blade / lower outline of the plate
ARC_CX, ARC_CZ, ARC_R = 87.3, -116.1, 112.5
BLADE_KNEE_Z = -24.6           # left edge goes vertical down to here
BLADE_DIR = (-0.30, -0.95)      # direction of the slanted blade edge
TIP_R = 1.2

# upper arm
ARM_Y0 = 25.8                  # arm front face
TAB_TOP = 63.0
TAB_BOT = 54.4
TAB_X1 = 104.75
ARM_SLOPE_X0 = 35.5            # where the 45 deg face meets the box top
ARM_IN_R = 7.0                 # inner fillet
TAB_R_FRONT = 6.0
TAB_R_BACK = 6.0
ARM_TOP_R = 5.0
ARM_FOOT_R = 4.0

# ramp in front of the arm
RAMP_Y0 = 16.8
RAMP_R = 5.0

# right wall window
WIN_Y1 = 31.5
WIN_Z0 = 11.0
WIN_Z1 = 33.1
WIN_R = 3.0

# lower bracket (plate extension right of the box, shelf, boss)
BR_X1 = 108.0                  # right end of the plate
BR_TOP = 16.55                 # top of bracket plate / boss
BR_CH = 2.2                    # corner chamfers of the bracket plate outline
SHELF_Z0 = 1.9                 # horizontal shelf
SHELF_Z1 = 4.4
LWALL_X1 = 71.65               # short side wall next to the box
LWALL_Y0 = 37.9
LW_CH = 2.5                    # chamfer on its front-top edge
BLOCK_X0, BLOCK_X1 = 87.0, 95.0
BLOCK_Y0 = 39.6
AXIS_X, AXIS_Y = 87.0, 40.2    # shaft axis (boss + big tab hole)
BOSS_R = 7.1
BOSS_HOLE_D = 5.3
BOSS_FOOT_R = 2.2
BR_FCH = 2.5                   # 45 deg fillet strips shelf/plate, shelf/wall
BR_VCH = 1.0                   # vertical 45 deg strips in the inner corners

# bar
BAR_X0, BAR_X1 = 85.15, 88.85
BAR_Y0, BAR_Y1 = 6.2, 25.5
BAR_Z0, BAR_Z1 = -2.25, 7.8

# tooth under the box
TOOTH_Y0, TOOTH_Y1 = 6.15, 25.4

HOLE_S = 2.4     # plate holes
HOLE_W = 2.6     # right wall holes
HOLE_B = 2.6     # holes near the lower edge
NOTCH_X = (72.4, 100.9)
NOTCH_Z = -2.9
CB_D = 4.0
CB_DEPTH = 1.5


def prism_xz(pts, y0, y1):
    return cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close().extrude(y1 - y0)


def prism_yz(pts, x0, x1):
    return cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)


def prism_xy(pts, z0, z1):
    return cq.Workplane("XY", origin=(0, 0, z0)).polyline(pts).close().extrude(z1 - z0)


def try_fillet(wp, p0, p1, r):
    """fillet edges whose centre lies inside the box p0-p1 (keeps the solid if it fails)"""
    try:
        out = wp.edges(cq.selectors.BoxSelector(p0, p1)).fillet(r)
        if out.val().isValid():
            return out
    except Exception:
        pass
    return wp


def try_chamfer(wp, p0, p1, c):
    try:
        out = wp.edges(cq.selectors.BoxSelector(p0, p1)).chamfer(c)
        if out.val().isValid():
            return out
    except Exception:
        pass
    return wp


# ---------------- back plate outline ----------------
# slanted blade edge: from knee K along BLADE_DIR until it meets the big arc,
# the sharp tip is rounded with TIP_R
kx, kz = 0.0, BLADE_KNEE_Z
ul = math.hypot(*BLADE_DIR)
ux, uz = BLADE_DIR[0] / ul, BLADE_DIR[1] / ul
nx, nz = -uz, ux          # normal pointing into the plate (to +X side)
if nx < 0:
    nx, nz = -nx, -nz
# centre c = K + s*u + TIP_R*n, |c - O| = R + TIP_R
px, pz = kx + TIP_R * nx - ARC_CX, kz + TIP_R * nz - ARC_CZ
b = 2 * (px * ux + pz * uz)
c = px * px + pz * pz - (ARC_R + TIP_R) ** 2
s = (-b - math.sqrt(b * b - 4 * c)) / 2.0
if s < 0:
    s = (-b + math.sqrt(b * b - 4 * c)) / 2.0
tcx, tcz = kx + s * ux + TIP_R * nx, kz + s * uz + TIP_R * nz
t_line = (kx + s * ux, kz + s * uz)
dd = math.hypot(tcx - ARC_CX, tcz - ARC_CZ)
t_arc = (ARC_CX + (tcx - ARC_CX) * ARC_R / dd, ARC_CZ + (tcz - ARC_CZ) * ARC_R / dd)
mx, mz = (t_line[0] - tcx) + (t_arc[0] - tcx), (t_line[1] - tcz) + (t_arc[1] - tcz)
ml = math.hypot(mx, mz)
t_mid = (tcx + TIP_R * mx / ml, tcz + TIP_R * mz / ml)

arc_right_z = ARC_CZ + math.sqrt(ARC_R ** 2 - (BR_X1 - ARC_CX) ** 2)
a0 = math.atan2(arc_right_z - ARC_CZ, BR_X1 - ARC_CX)
a1 = math.atan2(t_arc[1] - ARC_CZ, t_arc[0] - ARC_CX)
am = 0.5 * (a0 + a1)
arc_mid = (ARC_CX + ARC_R * math.cos(am), ARC_CZ + ARC_R * math.sin(am))

plate = (
    cq.Workplane("XZ", origin=(0, PY1, 0))
    .moveTo(0, BOX_H)
    .lineTo(BOX_W, BOX_H)
    .lineTo(BOX_W, BR_TOP + BR_CH)
    .lineTo(BOX_W + BR_CH, BR_TOP)
    .lineTo(BR_X1 - 2.0, BR_TOP)
    .lineTo(BR_X1, BR_TOP - 2.0)
    .lineTo(BR_X1, arc_right_z)
    .threePointArc(arc_mid, t_arc)
    .threePointArc(t_mid, t_line)
    .lineTo(kx, kz)
    .close()
    .extrude(PLATE_T)
)

# ---------------- box outer + plate ----------------
base = cq.Workplane("XY").box(BOX_W, PY1, BOX_H, centered=False).union(plate)
base = try_chamfer(base, (-0.1, -0.1, BOX_H - 0.1), (0.1, PY1 + 0.1, BOX_H + 0.1), BOX_C)          # top-left
base = try_chamfer(base, (BOX_W - 0.1, -0.1, BOX_H - 0.1), (BOX_W + 0.1, PY1 + 0.1, BOX_H + 0.1), BOX_C)  # top-right
base = try_chamfer(base, (-0.1, -0.1, -0.1), (0.1, PY0 + 0.1, 0.1), BOX_C)                      # bottom-left
base = try_chamfer(base, (BOX_W - 0.1, -0.1, -0.1), (BOX_W + 0.1, PY0 + 0.1, 0.1), BOX_C)       # bottom-right

# ---------------- arm ----------------
x0 = ARM_SLOPE_X0
arm = (
    cq.Workplane("XZ", origin=(0, PY1, 0))
    .moveTo(x0, BOX_H)
    .lineTo(x0 + (TAB_TOP - BOX_H), TAB_TOP)
    .lineTo(TAB_X1, TAB_TOP)
    .lineTo(TAB_X1, TAB_BOT)
    .lineTo(BOX_W + ARM_IN_R, TAB_BOT)
    .threePointArc((BOX_W + ARM_IN_R - ARM_IN_R * math.sin(math.pi / 4),
                    TAB_BOT - ARM_IN_R + ARM_IN_R * math.cos(math.pi / 4)),
                   (BOX_W, TAB_BOT - ARM_IN_R))
    .lineTo(BOX_W, BOX_H - BOX_C)
    .lineTo(BOX_W - BOX_C, BOX_H)
    .close()
    .extrude(PY1 - ARM_Y0)
)
# round tab end in plan
arm = try_fillet(arm, (TAB_X1 - 0.1, ARM_Y0 - 0.1, TAB_BOT), (TAB_X1 + 0.1, ARM_Y0 + 0.1, TAB_TOP), TAB_R_FRONT)
arm = try_fillet(arm, (TAB_X1 - 0.1, PY1 - 0.1, TAB_BOT), (TAB_X1 + 0.1, PY1 + 0.1, TAB_TOP), TAB_R_BACK)
# round top of the sloped face
xt = x0 + (TAB_TOP - BOX_H)
arm = try_fillet(arm, (xt - 0.1, ARM_Y0, TAB_TOP - 0.1), (xt + 0.1, PY1, TAB_TOP + 0.1), ARM_TOP_R)

# ---------------- ramp (hip-roof gusset in front of the arm) ----------------
# left face: X = Z - a_off (continues the arm slope),
# right face: X = BOX_W + BOX_H - BOX_C - Z (same plane as the box edge chamfer)
a_off = BOX_H - ARM_SLOPE_X0
apex_z = (BOX_W + BOX_H - BOX_C + a_off) / 2.0
roof = prism_xz([(ARM_SLOPE_X0, BOX_H), (BOX_W - BOX_C, BOX_H), (apex_z - a_off, apex_z)],
                RAMP_Y0 - 1, ARM_Y0 + 1.0)
wedge_top = BOX_H + (ARM_Y0 - RAMP_Y0)
wedge = prism_yz([(RAMP_Y0, BOX_H), (ARM_Y0 + 1.0, BOX_H), (ARM_Y0 + 1.0, wedge_top + 1.0)],
                 ARM_SLOPE_X0 - 5, BOX_W + 5)
ramp = roof.intersect(wedge)

body = base.union(arm).union(ramp).clean()
# concave foot of the sloped face (arm + ramp)
body = try_fillet(body, (x0 - 0.1, RAMP_Y0 - 0.5, BOX_H - 0.1), (x0 + 0.1, PY1 + 0.5, BOX_H + 0.1), ARM_FOOT_R)
# blend ramp into arm front face
body = try_fillet(body, (x0, ARM_Y0 - 0.2, wedge_top - 0.3), (BOX_W, ARM_Y0 + 0.2, wedge_top + 0.3), RAMP_R)

# ---------------- hollow box + window ----------------
inner = cq.Workplane("XY").box(BOX_W - WALL_L - WALL_R, CAV_D + 1, BOX_H - WALL_T - WALL_B,
                               centered=False).translate((WALL_L, -1, WALL_B))
body = body.cut(inner)

c45 = math.cos(math.pi / 4)
win = (
    cq.Workplane("YZ", origin=(BOX_W - WALL_R - 1, 0, 0))
    .moveTo(-1, WIN_Z0 - WIN_R)
    .lineTo(0, WIN_Z0 - WIN_R)
    .threePointArc((WIN_R * (1 - c45), WIN_Z0 - WIN_R * (1 - c45)), (WIN_R, WIN_Z0))
    .lineTo(WIN_Y1 - WIN_R, WIN_Z0)
    .threePointArc((WIN_Y1 - WIN_R + WIN_R * c45, WIN_Z0 + WIN_R - WIN_R * c45), (WIN_Y1, WIN_Z0 + WIN_R))
    .lineTo(WIN_Y1, WIN_Z1 - WIN_R)
    .threePointArc((WIN_Y1 - WIN_R + WIN_R * c45, WIN_Z1 - WIN_R + WIN_R * c45), (WIN_Y1 - WIN_R, WIN_Z1))
    .lineTo(WIN_R, WIN_Z1)
    .threePointArc((WIN_R * (1 - c45), WIN_Z1 + WIN_R * (1 - c45)), (0, WIN_Z1 + WIN_R))
    .lineTo(-1, WIN_Z1 + WIN_R)
    .close()
    .extrude(WALL_R + 2)
)
body = body.cut(win)

# ---------------- bracket ----------------
shelf = prism_xy([(BOX_W - 0.5, 13.0), (79.25, 23.4), (90.75, 23.4), (BR_X1, 40.65),
                  (BR_X1, PY0 + 0.5), (BOX_W - 0.5, PY0 + 0.5)], SHELF_Z0, SHELF_Z1)
# side wall next to the box, top follows the plate chamfer, front-top edge chamfered
lw_top_in = BR_TOP + BR_CH
lw_top_out = BR_TOP + BR_CH - (LWALL_X1 - BOX_W)
lwall = prism_xz([(BOX_W - 0.5, SHELF_Z1 - 0.1), (LWALL_X1, SHELF_Z1 - 0.1),
                  (LWALL_X1, lw_top_out), (BOX_W - 0.5, lw_top_in)],
                 LWALL_Y0, PY0 + 0.5)
lw_cut = prism_yz([(LWALL_Y0 - 1, lw_top_in - LW_CH - 1), (LWALL_Y0 + LW_CH + 1.5, lw_top_in + 1.5),
                   (LWALL_Y0 - 1, lw_top_in + 1.5)], BOX_W - 1, LWALL_X1 + 1)
lwall = lwall.cut(lw_cut)
# block behind the right half of the boss
block = cq.Workplane("XY").box(BLOCK_X1 - BLOCK_X0, PY0 - BLOCK_Y0 + 0.5, BR_TOP - SHELF_Z1 + 0.1,
                               centered=False).translate((BLOCK_X0, BLOCK_Y0, SHELF_Z1 - 0.1))
boss = cq.Workplane("XY", origin=(AXIS_X, AXIS_Y, SHELF_Z1 - 0.1)).circle(BOSS_R).extrude(BR_TOP - SHELF_Z1 + 0.1)
# 45 deg fillets (chamfer strips) in the inside corners
ch_back = prism_yz([(PY0 + 0.2, SHELF_Z1 - 0.1), (PY0 - BR_FCH, SHELF_Z1 - 0.1), (PY0 + 0.2, SHELF_Z1 + BR_FCH + 0.2)],
                   LWALL_X1 - 0.2, BR_X1)
ch_side = prism_xz([(LWALL_X1 - 0.2, SHELF_Z1 - 0.1), (LWALL_X1 + BR_FCH, SHELF_Z1 - 0.1),
                    (LWALL_X1 - 0.2, SHELF_Z1 + BR_FCH + 0.2)], LWALL_Y0, PY0 + 0.2)
ch_v1 = prism_xy([(LWALL_X1 - 0.2, PY0 - BR_VCH), (LWALL_X1 - 0.2, PY0 + 0.2), (LWALL_X1 + BR_VCH + 0.2, PY0 + 0.2)],
                 SHELF_Z1 - 0.1, BR_TOP)
ch_v2 = prism_xy([(BLOCK_X1 - 0.2, PY0 - BR_VCH), (BLOCK_X1 - 0.2, PY0 + 0.2), (BLOCK_X1 + BR_VCH + 0.2, PY0 + 0.2)],
                 SHELF_Z1 - 0.1, BR_TOP)
brk = shelf.union(lwall).union(ch_back).union(ch_side).union(ch_v1).union(ch_v2).union(block).union(boss)
# concave flare at the foot of the boss (revolved profile)
f = BOSS_FOOT_R
flare = (
    cq.Workplane("XZ")
    .moveTo(BOSS_R - 0.3, SHELF_Z1 - 0.1)
    .lineTo(BOSS_R + f, SHELF_Z1 - 0.1)
    .lineTo(BOSS_R + f, SHELF_Z1)
    .threePointArc((BOSS_R + f - f * c45, SHELF_Z1 + f - f * c45), (BOSS_R, SHELF_Z1 + f))
    .lineTo(BOSS_R - 0.3, SHELF_Z1 + f)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((AXIS_X, AXIS_Y, 0))
)
brk = brk.union(flare)
# keep the bracket features in front of the plate
brk = brk.cut(cq.Workplane("XY").box(200, 20, 200).translate((50, PY0 + 0.3 + 10, 0)))

bar = cq.Workplane("XY").box(BAR_X1 - BAR_X0, BAR_Y1 - BAR_Y0, BAR_Z1 - BAR_Z0,
                             centered=False).translate((BAR_X0, BAR_Y0, BAR_Z0))

# tooth under box
tooth = prism_xz([(41.9, 0.5), (49.4, 0.5), (48.6, -7.95), (45.25, -8.75)], TOOTH_Y0, TOOTH_Y1)

# ---------------- combine ----------------
result = body.union(brk).union(bar).union(tooth)

# ---------------- holes ----------------
# boss / shaft axis (blind, stops at the shelf)
result = result.cut(cq.Workplane("XY", origin=(AXIS_X, AXIS_Y, SHELF_Z1)).circle(BOSS_HOLE_D / 2)
                    .extrude(BR_TOP - SHELF_Z1 + 1))
# tab holes (coaxial with the boss)
for x, d in [(78.3, 2.3), (AXIS_X, 5.3), (95.95, 2.3)]:
    result = result.cut(cq.Workplane("XY", origin=(x, AXIS_Y, TAB_BOT - 1)).circle(d / 2)
                        .extrude(TAB_TOP - TAB_BOT + 2))
# plate holes (through along Y)
for x, z, y0, d in [(64.5, 58.6, ARM_Y0 - 1, HOLE_S), (64.5, 12.1, CAV_D - 1, HOLE_S), (103.6, 12.1, PY0 - 1, HOLE_S)]:
    result = result.cut(cq.Workplane("XZ", origin=(0, PY1 + 1, 0)).center(x, z).circle(d / 2)
                        .extrude(PY1 + 1 - y0))
# holes close to the lower edge; their counterbores on the back face break through the edge
for x in NOTCH_X:
    result = result.cut(cq.Workplane("XZ", origin=(0, PY1 + 1, 0)).center(x, NOTCH_Z).circle(HOLE_B / 2)
                        .extrude(PY1 + 1 - (PY0 - 1)))
    result = result.cut(cq.Workplane("XZ", origin=(0, PY1 + 1, 0)).center(x, NOTCH_Z).circle(CB_D / 2)
                        .extrude(1 + CB_DEPTH))
# right wall holes (along X)
for y, z in [(6.25, 35.9), (33.5, 35.9), (6.25, 8.75), (33.5, 8.75)]:
    result = result.cut(cq.Workplane("YZ", origin=(BOX_W - WALL_R - 1, 0, 0)).center(y, z)
                        .circle(HOLE_W / 2).extrude(WALL_R + 2))

VIEW = {"azimuth": 45, "elevation": 26}
